"""Cup-shaped holder with a thick rounded back wall carrying a T-slot.

The body is a box with large rounded corners at the -X (back) end and small
ones at the +X end, a filleted bottom and an open-topped pocket.  The thick
back wall is split by a T-shaped slot (narrow neck at the outer face, wider
head inside) that opens into the pocket.  The slot floor has a small raised
lip under the neck, a slightly lower floor under the head, and ends in a drop
to the pocket floor flanked by two small rounded corner blocks.
"""
import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
L = 50.0          # overall length along X
W = 40.0          # overall width along Y
H = 38.0          # overall height along Z
R_OUT_BACK = 9.8  # big outer corner radius at the -X end
R_OUT_FRONT = 1.8 # small outer corner radius at the +X end
WALL = 1.95       # side / end wall thickness
FLOOR = 2.0       # bottom thickness of the pocket
BACK = 12.15      # thickness of the thick -X wall (pocket starts here)
BOT_FILLET = 1.8 # fillet around the bottom edges

NECK_HW = 6.7     # half width of the slot neck (outer opening)
NECK_D = 2.0      # depth of the neck along X
HEAD_HW = 7.6     # half width of the slot head (inside)
LIP_Z = 5.4       # height of the slot floor under the neck (outer lip)
HEAD_Z = 4.7      # height of the slot floor under the head
SLOT_FLOOR_END = 10.2  # X where the slot floor ends
BLOCK_IN = 5.65   # inner Y edge of the small corner blocks
BLOCK_TOP = 8.5   # top of the small corner blocks
BLOCK_R = 1.1     # rounding of the block corner

# pocket corner radius at the -X end: the arc runs tangentially into the slot head faces
R_IN_BACK = W / 2 - WALL - HEAD_HW


def rounded_profile(x0, x1, hw, r_back, r_front):
    """2D closed profile in XY: rectangle [x0,x1] x [-hw,hw] with
    radius r_back at the -X corners and r_front at the +X corners."""
    k = 1.0 - math.sqrt(0.5)
    wp = cq.Workplane("XY").moveTo(x0 + r_back, -hw)
    if r_front > 0:
        wp = wp.lineTo(x1 - r_front, -hw).threePointArc(
            (x1 - r_front * k, -hw + r_front * k), (x1, -hw + r_front))
        wp = wp.lineTo(x1, hw - r_front).threePointArc(
            (x1 - r_front * k, hw - r_front * k), (x1 - r_front, hw))
    else:
        wp = wp.lineTo(x1, -hw).lineTo(x1, hw)
    wp = wp.lineTo(x0 + r_back, hw).threePointArc(
        (x0 + r_back * k, hw - r_back * k), (x0, hw - r_back))
    wp = wp.lineTo(x0, -hw + r_back).threePointArc(
        (x0 + r_back * k, -hw + r_back * k), (x0 + r_back, -hw))
    return wp.close()


# outer body
body = rounded_profile(0, L, W / 2, R_OUT_BACK, R_OUT_FRONT).extrude(H)
body = body.faces("<Z").edges().fillet(BOT_FILLET)

# main pocket
pocket = rounded_profile(BACK, L - WALL, W / 2 - WALL, R_IN_BACK, 0).extrude(H).translate((0, 0, FLOOR))
body = body.cut(pocket)

# T-slot through the thick back wall, open to the pocket
neck = (cq.Workplane("XY").box(NECK_D + 1.0, 2 * NECK_HW, H, centered=(False, True, False))
        .translate((-1.0, 0, LIP_Z)))
head = (cq.Workplane("XY").box(BACK + 1.0 - NECK_D, 2 * HEAD_HW, H, centered=(False, True, False))
        .translate((NECK_D, 0, BLOCK_TOP)))
head_low = (cq.Workplane("XY").box(SLOT_FLOOR_END - NECK_D, 2 * HEAD_HW, H, centered=(False, True, False))
            .translate((NECK_D, 0, HEAD_Z)))
body = body.cut(neck).cut(head).cut(head_low)

# drop from the slot floor down to the pocket floor between the two corner blocks
drop = (cq.Workplane("XY")
        .box(BACK + 1.0 - SLOT_FLOOR_END, 2 * BLOCK_IN, H, centered=(False, True, False))
        .translate((SLOT_FLOOR_END, 0, FLOOR)))
body = body.cut(drop)

# round the inner vertical corner of each block (where it meets the pocket wall)
for sy in (-1, 1):
    body = body.edges(cq.selectors.BoxSelector(
        (BACK - 0.2, sy * BLOCK_IN - 0.2, FLOOR + 0.5),
        (BACK + 0.2, sy * BLOCK_IN + 0.2, BLOCK_TOP - 0.5))).fillet(BLOCK_R)

result = body
